import math
import cadquery as cq
from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections

# ---------------- driving dimensions (mm) ----------------
H = 100.0            # overall height (top of the tall half)

# barrel body: slightly "squarish" super-elliptical sections, lofted smoothly.
# (z, +X half-width, -X half-width, +Y half-width, -Y half-width,
#  super-ellipse exponents of the quadrants (+X+Y, +X-Y, -X+Y, -X-Y))
BODY_SECTIONS = [
    (0.0, 20.6, 20.95, 20.35, 20.85, (2.46, 2.35, 2.09, 2.04)),
    (21.0, 21.65, 22.0, 21.55, 21.85, (2.46, 2.35, 2.09, 2.04)),
    (42.0, 21.05, 21.7, 21.3, 21.85, (2.42, 2.32, 2.09, 2.04)),
    (63.0, 19.8, 19.8, 19.9, 21.3, (2.25, 2.2, 2.09, 2.04)),
    (84.0, 18.8, 18.6, 17.6, 20.45, (2.1, 2.05, 2.09, 2.04)),
    (105.0, 18.3, 18.0, 15.5, 19.6, (2.0, 2.0, 2.09, 2.04)),
]
N_SECTION_PTS = 16   # interpolation points per section spline

# +X top round (front view): arc of radius FR_R centred at (FR_X, FR_Z)
FR_R = 14.0
FR_X = 4.6
FR_Z = H - FR_R

# slanted cut on the -X half:  z = P_Z0 - P_SLOPE * y
P_Z0 = 56.0
P_SLOPE = 1.13

# cross hole through the tall half (along X)
HOLE_Y = -5.0
HOLE_Z = 92.7
HOLE_D = 4.0

# two shallow blind holes in the base
BASE_HOLE_X = 9.2
BASE_HOLE_D = 4.0
BASE_HOLE_DEPTH = 6.0

BIG = 80.0


def section_wire(z, ax_p, ax_n, by_p, by_n, expo):
    """closed spline through a quadrant-wise super-ellipse, seam at -X"""
    pts = []
    for i in range(N_SECTION_PTS):
        t = math.pi + 2.0 * math.pi * i / N_SECTION_PTS
        c, s = math.cos(t), math.sin(t)
        a = ax_p if c >= 0 else ax_n
        b = by_p if s >= 0 else by_n
        n = expo[(0 if c >= 0 else 2) + (0 if s >= 0 else 1)]
        x = a * math.copysign(abs(c) ** (2.0 / n), c)
        y = b * math.copysign(abs(s) ** (2.0 / n), s)
        pts.append(cq.Vector(x, y, z))
    edge = cq.Edge.makeSpline(pts, periodic=True)
    return cq.Wire.assembleEdges([edge])


# ---------------- barrel body (smooth loft) ----------------
wires = [section_wire(*sec) for sec in BODY_SECTIONS]
_loft = BRepOffsetAPI_ThruSections(True, False, 1e-6)
_loft.SetMaxDegree(3)           # cubic through the sections (smooth, well meshed)
for _w in wires:
    _loft.AddWire(_w.wrapped)
_loft.Build()
body = cq.Workplane("XY").add(cq.Solid(_loft.Shape()))

# ---------------- front profile (XZ) extruded along Y : rounds the +X top ----------------
_a45 = math.radians(45)
front = (
    cq.Workplane("XZ", origin=(0, BIG / 2, 0))      # normal -Y
    .moveTo(-30, -5)
    .lineTo(30, -5)
    .lineTo(30, 70)
    .lineTo(FR_X + FR_R, FR_Z)
    .threePointArc((FR_X + FR_R * math.cos(_a45), FR_Z + FR_R * math.sin(_a45)), (FR_X, H))
    .lineTo(-30, H)
    .close()
    .extrude(BIG)
)

# ---------------- side profile (YZ) extruded along X : sloped / rounded top ----------------
# +Y slope (from the +Y flank up to the ridge) and -Y round (from the ridge down)
SIDE_RIDGE = (-4.4, H)
side_slope = [
    (19.3, 66.0), (18.6, 71.0), (18.1, 74.1), (17.1, 78.0), (14.5, 83.2),
    (11.3, 87.8), (8.0, 91.7), (4.8, 94.9), (1.5, 97.5), (-1.7, 99.5),
    SIDE_RIDGE,
]
side_round = [
    (-7.4, 99.6), (-12.7, 97.4), (-15.9, 94.9), (-19.2, 88.4),
    (-20.6, 80.3), (-21.4, 72.0), (-22.4, 62.0),
]
side = (
    cq.Workplane("YZ", origin=(-BIG / 2, 0, 0))     # normal +X
    .moveTo(-30, -5)
    .lineTo(30, -5)
    .lineTo(30, 50)
    .lineTo(20.4, 60.0)
    .spline(side_slope, includeCurrent=True)
    .spline(side_round, includeCurrent=True)
    .lineTo(-30, 55)
    .close()
    .extrude(BIG)
)

part = body.intersect(front).intersect(side)

# ---------------- slanted plane cut on the -X half ----------------
nrm = cq.Vector(0, P_SLOPE, 1).normalized()
cut_plane = cq.Plane(origin=(0, 0, P_Z0), xDir=(1, 0, 0), normal=nrm.toTuple())
cutter = (
    cq.Workplane(cut_plane)
    .center(-BIG / 2, 0)
    .rect(BIG, 3 * BIG)
    .extrude(2 * BIG)
)
part = part.cut(cutter)

# ---------------- cross hole along X ----------------
hole = (
    cq.Workplane("YZ", origin=(-BIG / 2, 0, 0))
    .center(HOLE_Y, HOLE_Z)
    .circle(HOLE_D / 2)
    .extrude(BIG)
)
part = part.cut(hole)

# ---------------- base holes ----------------
base_holes = (
    cq.Workplane("XY")
    .pushPoints([(BASE_HOLE_X, 0), (-BASE_HOLE_X, 0)])
    .circle(BASE_HOLE_D / 2)
    .extrude(BASE_HOLE_DEPTH)
)
part = part.cut(base_holes)

result = part
VIEW = {"azimuth": 45, "elevation": 26}
